import cadquery as cq
import math

# ---- driving dimensions (mm) ----
D = 50.0          # cup outer diameter
H = 29.0          # cup height
WALL = 1.0        # cup wall thickness
FLOOR = 1.0       # floor thickness
GAP = 4.0         # gap between neighbouring cups
HOLE_D = 7.5      # central hole in each floor
RIB_T = 2.2       # rib thickness
RIB_H = 14.5      # depth of the rib web in the middle (measured down from the rim)
LEG_L = 5.3       # length of the full-height rib "legs" next to each cup wall
N = 3             # cups per row / column

R = D / 2.0
P = D + GAP       # pitch
offs = [(i - (N - 1) / 2.0) * P for i in range(N)]
centers = [(x, y) for x in offs for y in offs]


def cylinder(x, y, r, z0, h, seam_deg):
    """Vertical cylinder with its seam edge turned to seam_deg."""
    return (cq.Workplane("XY").workplane(offset=z0)
            .transformed(offset=(x, y, 0), rotate=(0, 0, seam_deg))
            .circle(r).extrude(h))


def outer_seam(x, y):
    # put the seam line where the six standard views do not show it
    if x > 0 and y < 0:
        return 135.0
    if y < 0:
        return 45.0
    return 225.0


# outer cylinders
body = None
for (x, y) in centers:
    c = cylinder(x, y, R, 0, H, outer_seam(x, y))
    body = c if body is None else body.union(c)

# X-shaped ribs in the gaps between every 2x2 group of cups.
# Each rib is a full-height web with a rectangular notch cut from the
# bottom in its middle, leaving short full-height legs at the cup walls.
span = P * math.sqrt(2) - 2 * R                  # clear distance wall to wall
rib_len = P * math.sqrt(2) - 2 * (R - WALL) + 2.0
notch_len = span - 2 * LEG_L
notch_h = H - RIB_H
gaps = [(offs[k] + offs[k + 1]) / 2 for k in range(N - 1)]
for gx in gaps:
    for gy in gaps:
        for ang in (45, -45):
            wp = (cq.Workplane("XY")
                  .transformed(offset=(gx, gy, 0), rotate=(0, 0, ang)))
            web = wp.rect(rib_len, RIB_T).extrude(H)
            notch = (cq.Workplane("XY")
                     .transformed(offset=(gx, gy, -1), rotate=(0, 0, ang))
                     .rect(notch_len, RIB_T + 2).extrude(notch_h + 1))
            body = body.union(web.cut(notch))

# hollow out the cups (open top, floor at the bottom) and drill the floor holes
for (x, y) in centers:
    bore = cylinder(x, y, R - WALL, FLOOR, H, 45.0)
    hole = cylinder(x, y, HOLE_D / 2, -1, FLOOR + 2, 45.0)
    body = body.cut(bore).cut(hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
